import math
import cadquery as cq

# ---------------------------------------------------------------
# Robot-shaped kiosk figure: leg block, torso with shoulders,
# neck and a tilted monitor head.  X = width, Y = depth (+Y back),
# Z = up.  Units: mm.
# ---------------------------------------------------------------

# ---- leg (lower block) ----
LEG_HW = 21.0       # half width (X)
LEG_HD = 20.5       # half depth (Y)
LEG_H = 44.0        # height (overlaps into torso)
LEG_CH_Y = 8.0      # bottom front/back chamfer
LEG_CH_Z = 8.7
WHEEL_Z = 20.0
WHEEL_R = 19.0
WHEEL_GROOVE_D = 1.6
WHEEL_IN_R = 13.0
WHEEL_DEPTH = 3.0

# ---- lower torso ----
T_HW = 35.6
T_HD = 21.6
T_HD_TOP = 23.0
T_IN_HD = 21.3
T_IN_HD_BOT = 20.3
T_SIDE_HW_TOP = 14.5
T_SIDE_HW_BOT = 12.0
T_CORE_Z_BOT = 49.5
T_Z0 = 41.5
T_Z1 = 137.2
T_CH_X = 5.0
T_BOT_CH_X = 10.5
T_BOT_CH_Z = 10.5
T_BOT_CH_Y = 8.0

# ---- shoulder block ----
S_HW = 44.2
S_Z_TOP = 178.4
S_Z_TOP_OUT = 172.2
S_Z_SIDE_BOT = 139.5
S_Z_TAPER = 123.6
S_Z_BOTTOM = 105.0
S_HD = 24.0
S_LOW_HD = 21.3
S_TOP_CH_BACK = 6.5
S_TOP_CH_FRONT_Y = 9.0
S_FRONT_TOP_CH = 4.0
ST_POCK_X0, ST_POCK_X1 = 18.8, 23.5
ST_POCK_Y0, ST_POCK_Y1 = 4.2, 14.4
ST_POCK_D = 4.0
S_BACK_HX = 23.7
S_BACK_SIDE_Y = 18.6
S_FRONT_HX = 29.0
S_FRONT_Y = -21.3
S_FRONT_SIDE_Y = -17.7

# ---- shoulder side pocket + disc ----
SP_Y0, SP_Y1 = -16.5, 17.5
SP_Z0, SP_Z1 = 140.8, 171.0
SP_CH = 7.0
SP_DEPTH = 6.0
DISC_R = 14.0
DISC_Y = 1.0
DISC_Z = 155.5

# ---- front / back plates ----
CHEST_HW = 24.0
CHEST_Z0 = 135.4
CHEST_Z1 = 170.7
BAND_Z0 = 128.3
PLATE_HW = 24.0
PLATE_T = 1.0
PLATE_Z0 = 47.0
PANEL_HW = 22.6
PANEL_Z0 = 51.5
PANEL_BOT_XR = 12.1
PANEL_DEPTH = 1.2
SLOT_X = 0.0
SLOT_W = 5.0
SLOT_D = 2.0
SLOT_Z0 = 58.0
SLOT_Z1 = 118.0

# ---- neck ----
NECK_HW = 18.0
NECK_Y0 = -19.0
NECK_Y1 = 19.5
NECK_Z0 = 165.0
NECK_Z1 = 226.0

# ---- head ----
TILT = math.radians(8.0)
MON_W = 60.0
MON_H = 50.0
MON_T = 10.0
MON_T1 = 6.0
MON_INSET = 1.2
MON_R = 5.0
MON_Y = -26.5       # front-bottom edge
MON_Z = 188.0
SCREEN_W = 48.0
SCREEN_B = 18.0     # screen bottom above monitor bottom
SCREEN_H = 26.0
SCREEN_D = 1.5
HOUSE_BACK_Y = 19.5
HOUSE_BOT_Z = 187.0
HOUSE_TOP_CH = 2.0
HOUSE_FRONT_HX = 28.0
HOUSE_BACK_HX = 15.5
HOUSE_TAPER_Y = -10.2
HOUSE_CURVE_Z = 223.0
HOUSE_CURVE_R = 20.5


def poly_xz(pts, y0, y1):
    """Polygon in XZ extruded along Y from y0 to y1."""
    wp = cq.Workplane("XZ", origin=(0, y1, 0))
    return wp.polyline(pts).close().extrude(y1 - y0)


def poly_yz(pts, x0, x1):
    """Polygon in YZ extruded along X from x0 to x1."""
    wp = cq.Workplane("YZ", origin=(x0, 0, 0))
    return wp.polyline(pts).close().extrude(x1 - x0)


def poly_xy(pts, z0, z1):
    wp = cq.Workplane("XY", origin=(0, 0, z0))
    return wp.polyline(pts).close().extrude(z1 - z0)


def octagon(yc, zc, w, h, c):
    return [(yc - w / 2 + c, zc - h / 2), (yc + w / 2 - c, zc - h / 2), (yc + w / 2, zc - h / 2 + c),
            (yc + w / 2, zc + h / 2 - c), (yc + w / 2 - c, zc + h / 2), (yc - w / 2 + c, zc + h / 2),
            (yc - w / 2, zc + h / 2 - c), (yc - w / 2, zc - h / 2 + c)]


BIG = 200.0

# ================= leg =================
leg = cq.Workplane("XY").box(2 * LEG_HW, 2 * LEG_HD, LEG_H, centered=(True, True, False))
leg_side = poly_yz([(-LEG_HD, LEG_CH_Z), (-LEG_HD + LEG_CH_Y, 0), (LEG_HD - LEG_CH_Y, 0),
                    (LEG_HD, LEG_CH_Z), (LEG_HD, LEG_H), (-LEG_HD, LEG_H)], -BIG, BIG)
leg = leg.intersect(leg_side)

for sgn in (1, -1):
    x_face = sgn * LEG_HW
    wp = cq.Workplane("YZ", origin=(x_face, 0, 0))
    # bevelled groove around the wheel ring
    groove = (wp.center(0, WHEEL_Z).polygon(12, 2 * WHEEL_R)
              .extrude(-sgn * WHEEL_GROOVE_D))
    bevel = (cq.Workplane("YZ", origin=(x_face - sgn * WHEEL_GROOVE_D, 0, 0))
             .center(0, WHEEL_Z).polygon(12, 2 * WHEEL_R)
             .extrude(sgn * WHEEL_GROOVE_D, taper=45))
    leg = leg.cut(groove.cut(bevel))
    hexp = (wp.center(0, WHEEL_Z).polygon(8, 2 * WHEEL_IN_R)
            .extrude(-sgn * WHEEL_DEPTH))
    leg = leg.cut(hexp)

# ================= lower torso =================
tf = poly_xz([(-T_HW, T_Z0 + T_BOT_CH_Z), (-T_HW + T_BOT_CH_X, T_Z0),
              (T_HW - T_BOT_CH_X, T_Z0), (T_HW, T_Z0 + T_BOT_CH_Z),
              (T_HW, T_Z1), (-T_HW, T_Z1)], -BIG, BIG)
ts = poly_yz([(-T_HD, T_Z0 + T_BOT_CH_Y), (-T_HD + T_BOT_CH_Y, T_Z0), (T_HD - T_BOT_CH_Y, T_Z0),
              (T_HD, T_Z0 + T_BOT_CH_Y), (T_HD_TOP, T_Z1), (-T_HD_TOP, T_Z1)], -BIG, BIG)
torso_full = tf.intersect(ts)


def core_oct(z):
    """Octagonal cross-section of the torso core; it narrows slightly downwards."""
    f = (z - T_CORE_Z_BOT) / (T_Z1 - T_CORE_Z_BOT)
    hd = T_IN_HD_BOT + (T_IN_HD - T_IN_HD_BOT) * f
    sw = T_SIDE_HW_BOT + (T_SIDE_HW_TOP - T_SIDE_HW_BOT) * f
    return [(-T_HW + T_CH_X, -hd), (T_HW - T_CH_X, -hd), (T_HW, -sw), (T_HW, sw),
            (T_HW - T_CH_X, hd), (-T_HW + T_CH_X, hd), (-T_HW, sw), (-T_HW, -sw)]


def oct_wire(pts, z):
    return cq.Wire.makePolygon([cq.Vector(x, y, z) for x, y in pts], close=True)


# core of the lower torso (ruled loft) sits slightly behind the front/back plates
core = cq.Workplane("XY").add(cq.Solid.makeLoft(
    [oct_wire(core_oct(T_Z0), T_Z0), oct_wire(core_oct(T_Z1), T_Z1)], True))
ts_in = poly_yz([(-T_IN_HD, T_Z0 + T_BOT_CH_Y), (-T_HD + T_BOT_CH_Y, T_Z0),
                 (T_HD - T_BOT_CH_Y, T_Z0), (T_IN_HD, T_Z0 + T_BOT_CH_Y),
                 (40.0, T_Z1 + 5), (-40.0, T_Z1 + 5)], -BIG, BIG)
torso = core.intersect(tf).intersect(ts_in)
plates = torso_full.intersect(
    cq.Workplane("XY").box(2 * PLATE_HW, 100, T_Z1 - PLATE_Z0, centered=(True, True, False))
    .translate((0, 0, PLATE_Z0)))
torso = torso.union(plates)

# front lower panel recess
def t_face_y(z):
    z0 = T_Z0 + T_BOT_CH_Y
    return T_HD + (T_HD_TOP - T_HD) * (z - z0) / (T_Z1 - z0)


panel_box = poly_yz([(-t_face_y(PANEL_Z0) + PANEL_DEPTH, PANEL_Z0), (-40.0, PANEL_Z0),
                     (-40.0, BAND_Z0), (-t_face_y(BAND_Z0) + PANEL_DEPTH, BAND_Z0)],
                    -PANEL_HW, PANEL_HW)
# front panel outline: trapezoid with a slanted right-hand edge
panel = panel_box.intersect(
    poly_xz([(-PANEL_HW, PANEL_Z0), (PANEL_BOT_XR, PANEL_Z0),
             (PANEL_HW, BAND_Z0), (-PANEL_HW, BAND_Z0)], -BIG, BIG))
# back lower panel recess with vertical slot
bpanel = panel_box.mirror("XZ")
slot = poly_yz([(t_face_y(SLOT_Z0) - PANEL_DEPTH - SLOT_D, SLOT_Z0), (40.0, SLOT_Z0),
                (40.0, SLOT_Z1), (t_face_y(SLOT_Z1) - PANEL_DEPTH - SLOT_D, SLOT_Z1)],
               SLOT_X - SLOT_W / 2, SLOT_X + SLOT_W / 2)

# ================= shoulder block =================
# upper shoulder block (above the side taper)
sf = poly_xz([(-CHEST_HW, S_Z_TOP), (CHEST_HW, S_Z_TOP), (S_HW, S_Z_TOP_OUT),
              (S_HW, S_Z_SIDE_BOT), (-S_HW, S_Z_SIDE_BOT),
              (-S_HW, S_Z_TOP_OUT)], -BIG, BIG)
ss = poly_yz([(-S_LOW_HD, S_Z_BOTTOM), (S_LOW_HD, S_Z_BOTTOM), (S_LOW_HD, CHEST_Z0), (S_HD, CHEST_Z0),
              (S_HD, S_Z_TOP - S_TOP_CH_BACK),
              (S_HD - S_TOP_CH_BACK, S_Z_TOP), (-S_HD + S_TOP_CH_FRONT_Y, S_Z_TOP),
              (-S_HD, CHEST_Z1), (-S_HD, CHEST_Z0), (-S_LOW_HD, CHEST_Z0)], -BIG, BIG)
sp = poly_xy([(-S_FRONT_HX, S_FRONT_Y), (S_FRONT_HX, S_FRONT_Y), (S_HW, S_FRONT_SIDE_Y),
              (S_HW, S_BACK_SIDE_Y), (S_BACK_HX, S_HD), (-S_BACK_HX, S_HD),
              (-S_HW, S_BACK_SIDE_Y), (-S_HW, S_FRONT_SIDE_Y)], 0, 300)
shoulder = sf.intersect(ss).intersect(sp)


# chamfer along the front-top edge of each shoulder (plane cut)
def v_add(a, b, k=1.0):
    return (a[0] + k * b[0], a[1] + k * b[1], a[2] + k * b[2])


def v_cross(a, b):
    return (a[1] * b[2] - a[2] * b[1], a[2] * b[0] - a[0] * b[2], a[0] * b[1] - a[1] * b[0])


def z_top(x):
    return S_Z_TOP - (abs(x) - CHEST_HW) * (S_Z_TOP - S_Z_TOP_OUT) / (S_HW - CHEST_HW)


for sgn in (1, -1):
    ea = (sgn * S_FRONT_HX, S_FRONT_Y, z_top(S_FRONT_HX))
    eb = (sgn * S_HW, S_FRONT_SIDE_Y, S_Z_TOP_OUT)
    ed = (eb[0] - ea[0], eb[1] - ea[1], eb[2] - ea[2])
    # inward direction on the top face, perpendicular to the edge
    fn = (S_FRONT_SIDE_Y - S_FRONT_Y, -(S_HW - S_FRONT_HX), 0.0)
    fl = math.hypot(fn[0], fn[1])
    back = (-sgn * fn[0] / fl, -fn[1] / fl, 0.0)
    back = (back[0], back[1], -(S_Z_TOP - S_Z_TOP_OUT) / (S_HW - CHEST_HW) * back[0] * sgn)
    p1 = v_add(ea, (0, 0, -S_FRONT_TOP_CH))
    p2 = v_add(eb, (0, 0, -S_FRONT_TOP_CH))
    p3 = v_add(ea, back, S_FRONT_TOP_CH)
    nrm = v_cross((p2[0] - p1[0], p2[1] - p1[1], p2[2] - p1[2]),
                  (p3[0] - p1[0], p3[1] - p1[1], p3[2] - p1[2]))
    mid = v_add(ea, ed, 0.5)
    side = sum((mid[i] - p1[i]) * nrm[i] for i in range(3))
    if side < 0:
        nrm = (-nrm[0], -nrm[1], -nrm[2])
    cut_pl = cq.Plane(origin=p1, xDir=ed, normal=nrm)
    shoulder = shoulder.cut(cq.Workplane(cut_pl).rect(300, 300).extrude(60))

# small pockets in the shoulder top on either side of the neck
for sgn in (1, -1):
    sp_cut = (cq.Workplane("XY")
              .box(ST_POCK_X1 - ST_POCK_X0, ST_POCK_Y1 - ST_POCK_Y0, ST_POCK_D + 5.0,
                   centered=(False, False, False))
              .translate((ST_POCK_X0 if sgn > 0 else -ST_POCK_X1, ST_POCK_Y0, S_Z_TOP - ST_POCK_D)))
    shoulder = shoulder.cut(sp_cut)

# lower shoulder: ruled loft from the shoulder plan down to the torso plan
sp_pts = [(-S_FRONT_HX, S_FRONT_Y), (S_FRONT_HX, S_FRONT_Y), (S_HW, S_FRONT_SIDE_Y),
          (S_HW, S_BACK_SIDE_Y), (S_BACK_HX, S_HD), (-S_BACK_HX, S_HD),
          (-S_HW, S_BACK_SIDE_Y), (-S_HW, S_FRONT_SIDE_Y)]
tp_pts = [(x * 0.995, y * 0.99) for x, y in core_oct(S_Z_TAPER)]  # just inside the core
w_top = cq.Wire.makePolygon([cq.Vector(x, y, S_Z_SIDE_BOT) for x, y in sp_pts], close=True)
w_bot = cq.Wire.makePolygon([cq.Vector(x, y, S_Z_TAPER) for x, y in tp_pts], close=True)
s_low = cq.Workplane("XY").add(cq.Solid.makeLoft([w_bot, w_top], True))
s_low = s_low.intersect(ss)
shoulder = shoulder.union(s_low)

# chest plate (raised panel on the front)
chest_side = poly_yz([(-S_HD, CHEST_Z0), (S_FRONT_Y + 0.5, CHEST_Z0), (S_FRONT_Y + 0.5, S_Z_TOP),
                      (-S_HD + S_TOP_CH_FRONT_Y, S_Z_TOP), (-S_HD, CHEST_Z1)],
                     -CHEST_HW, CHEST_HW)
chest = chest_side

# side pockets with disc
for sgn in (1, -1):
    wp = cq.Workplane("YZ", origin=(sgn * S_HW, 0, 0))
    pts = octagon(0.5 * (SP_Y0 + SP_Y1), 0.5 * (SP_Z0 + SP_Z1), SP_Y1 - SP_Y0, SP_Z1 - SP_Z0, SP_CH)
    pocket = wp.polyline(pts).close().extrude(-sgn * SP_DEPTH)
    shoulder = shoulder.cut(pocket)
    disc = (cq.Workplane("YZ", origin=(sgn * (S_HW - SP_DEPTH), 0, 0))
            .center(DISC_Y, DISC_Z).circle(DISC_R).extrude(sgn * (SP_DEPTH - 1.0)))
    notch = (cq.Workplane("XY").box(20, 10, 12, centered=(True, False, True))
             .translate((sgn * S_HW, DISC_Y + 7.5, DISC_Z + 1.5)))
    disc = disc.cut(notch)
    shoulder = shoulder.union(disc)

# ================= neck =================
neck = poly_xy([(-NECK_HW, NECK_Y0), (NECK_HW, NECK_Y0), (HOUSE_BACK_HX, NECK_Y1),
                (-HOUSE_BACK_HX, NECK_Y1)], NECK_Z0, NECK_Z1)
head_plan = poly_xy([(-HOUSE_FRONT_HX, -60), (HOUSE_FRONT_HX, -60),
                     (HOUSE_FRONT_HX, HOUSE_TAPER_Y), (HOUSE_BACK_HX, HOUSE_BACK_Y),
                     (-HOUSE_BACK_HX, HOUSE_BACK_Y), (-HOUSE_FRONT_HX, HOUSE_TAPER_Y)], 0, 300)
# trapezoid recess in neck front
nrec = (cq.Workplane("XZ", origin=(0, NECK_Y0, 0))
        .polyline([(-13, 185.5), (13, 185.5), (11, 176.5), (-11, 176.5)]).close()
        .extrude(-4.0))
neck = neck.cut(nrec)
# pocket at back of neck
nback = (cq.Workplane("XY").box(24, 8, 17, centered=(True, True, False))
         .translate((0, NECK_Y1, 176)))
neck = neck.cut(nback)

# ================= head =================
st, ct = math.sin(TILT), math.cos(TILT)
fb = (0.0, MON_Y, MON_Z)   # front-bottom centre
ft = (0.0, MON_Y + MON_H * st, MON_Z + MON_H * ct)

mon_plane = cq.Plane(origin=(0, MON_Y + 0.5 * MON_H * st, MON_Z + 0.5 * MON_H * ct),
                     xDir=(1, 0, 0), normal=(0, -ct, st))
monitor = (cq.Workplane(mon_plane).sketch().rect(MON_W, MON_H).vertices().chamfer(MON_R)
           .finalize().extrude(-MON_T1))
mon_back = (cq.Workplane(mon_plane).workplane(offset=-MON_T1)
            .sketch().rect(MON_W - 2 * MON_INSET, MON_H - 2 * MON_INSET).vertices().chamfer(MON_R)
            .finalize().extrude(-(MON_T - MON_T1)))
monitor = monitor.union(mon_back)
screen = (cq.Workplane(mon_plane).center(0, -MON_H / 2 + SCREEN_B + SCREEN_H / 2)
          .rect(SCREEN_W, SCREEN_H).extrude(-SCREEN_D))
monitor = monitor.cut(screen)

# housing behind the monitor (side profile x plan taper)
z_back_top = ft[2] - (HOUSE_BACK_Y - ft[1]) * math.tan(TILT)
_d = MON_T - 1.0                      # housing starts inside the monitor
_a = (ft[1] + _d * ct, ft[2] - _d * st)  # top point on the monitor's back
_b = (fb[1] + _d * ct, fb[2] - _d * st)  # bottom point on the monitor's back
hp = (cq.Workplane("YZ", origin=(-BIG, 0, 0))
      .moveTo(*_a)
      .lineTo(HOUSE_BACK_Y - 2.0, z_back_top)
      .lineTo(HOUSE_BACK_Y, z_back_top - 2.0)
      .lineTo(HOUSE_BACK_Y, HOUSE_CURVE_Z)
      .threePointArc((HOUSE_BACK_Y - HOUSE_CURVE_R * math.sin(math.pi / 4),
                      HOUSE_CURVE_Z - HOUSE_CURVE_R + HOUSE_CURVE_R * math.cos(math.pi / 4)),
                     (HOUSE_BACK_Y - HOUSE_CURVE_R, HOUSE_CURVE_Z - HOUSE_CURVE_R))
      .lineTo(-5.5, HOUSE_BOT_Z)
      .lineTo(_b[0] + (HOUSE_BOT_Z - _b[1]) * st / ct, HOUSE_BOT_Z)
      .close()
      .extrude(2 * BIG))
# front outline of the housing: chamfered lower corners so it hides behind the monitor
_hc = 7.0
house_front = poly_xz([(-HOUSE_FRONT_HX + _hc, HOUSE_BOT_Z - 1), (HOUSE_FRONT_HX - _hc, HOUSE_BOT_Z - 1),
                       (HOUSE_FRONT_HX, HOUSE_BOT_Z + _hc - 1), (HOUSE_FRONT_HX, 300),
                       (-HOUSE_FRONT_HX, 300), (-HOUSE_FRONT_HX, HOUSE_BOT_Z + _hc - 1)], -BIG, BIG)
housing = hp.intersect(head_plan).intersect(house_front)
# chamfer the two edges between the sloped top and the tapered sides
housing = housing.edges(cq.selectors.BoxSelector((15.0, -8.0, 226.0), (27.0, 18.0, 240.0))
                        + cq.selectors.BoxSelector((-27.0, -8.0, 226.0), (-15.0, 18.0, 240.0))
                        ).chamfer(HOUSE_TOP_CH)

head = monitor.union(housing)

result = (leg.union(torso).union(shoulder).union(chest)
          .union(neck).union(head)
          .cut(panel).cut(bpanel).cut(slot))
